import math

import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# U-shaped bracket / tray: floor plate with a left wall, back wall and right wall
# wrapped round two rounded vertical corners, two grooves round the outside,
# ribs inside the side walls, cut-outs in the back wall, a countersunk pivot hole
# and countersunk arc slot in the floor, and the engraved marking "KV_2A".

# ---------------- driving dimensions (mm) ----------------
W = 120.0          # overall width (X), outer face to outer face of side walls
DF = 47.2          # floor depth (Y), front edge to outer face of back wall
H = 52.5           # overall height (Z)
TW = 2.6           # wall thickness
TF = 3.85          # floor thickness
RO = 7.5           # outer radius of the two vertical back corners
RI = RO - TW       # inner radius of the vertical back corners

# grooves running round the outside of the U-shaped wall
GROOVE_R = 1.3
GROOVE_Z = (8.5, 44.0)

# ribs on the inner face of the side walls
RIB_Z = (19.6, 22.7)     # rib centre heights
RIB_H = 1.0              # rib height (Z)
RIB_P = 1.2              # rib protrusion from the wall (X)
RIB_Y0, RIB_Y1 = -16.9, 11.6

# cut-outs in the back wall: (centre x, width, z bottom, z top)
BACK_CUTS = [
    (-43.0, 16.9, 21.3, 31.5),   # left rectangle
    (0.0, 13.9, 21.7, 34.2),     # centre square
    (0.0, 10.9, 35.9, 40.6),     # small slot above the square
    (40.1, 24.5, 21.3, 33.2),    # right wide rectangle
]
CUT_R = 0.5

# floor features
SLOT_X, SLOT_Y = -31.3, 0.5
SLOT_W, SLOT_L = 3.2, 21.5       # through slot (X width, Y length)
HOLE_X, HOLE_Y = 31.4, 0.5
HOLE_D = 3.9
CSK = 3.1                         # countersink depth of the slot (90 deg)
CSK_H = 2.7                       # countersink depth of the hole (90 deg)

TEXT_CAP = 13.0                   # cap height of the lettering
TEXT_STROKE = 1.2                 # stroke width of the lettering
TEXT_X0 = -20.1                   # x of the K stem centre line
TEXT_BASE_Y = -18.75              # baseline
TEXT_DEPTH = 0.6

YF = -DF / 2.0                    # floor front edge
YB = DF / 2.0                     # back outer face

# ---------------- main U-shaped tray ----------------
outer = (
    cq.Workplane("XY")
    .rect(W, DF)
    .extrude(H)
    .edges("|Z and >Y")
    .fillet(RO)
)

cavity = (
    cq.Workplane("XY")
    .center(0, (YF - 5.0 + YB - TW) / 2.0)
    .rect(W - 2 * TW, (YB - TW) - (YF - 5.0))
    .extrude(H + 2.0)
    .translate((0, 0, TF))
    .edges("|Z and >Y")
    .fillet(RI)
)
body = outer.cut(cavity)

# forward 45-degree tips of the side walls (outer corner forward)
for s in (-1, 1):
    xo = s * W / 2.0
    xi = s * (W / 2.0 - TW)
    tip = (
        cq.Workplane("XY")
        .polyline([(xo, YF), (xi, YF), (xo, YF - TW)])
        .close()
        .extrude(H)
    )
    body = body.union(tip)

# ---------------- grooves round the outside ----------------
ye = YF - TW - 3.0


def groove_path(z):
    return (
        cq.Workplane("XY", origin=(0, 0, z))
        .moveTo(-W / 2.0, ye)
        .lineTo(-W / 2.0, YB - RO)
        .radiusArc((-W / 2.0 + RO, YB), RO)
        .lineTo(W / 2.0 - RO, YB)
        .radiusArc((W / 2.0, YB - RO), RO)
        .lineTo(W / 2.0, ye)
    )


for gz in GROOVE_Z:
    prof = cq.Workplane("XZ", origin=(-W / 2.0, ye, gz)).circle(GROOVE_R)
    groove = prof.sweep(groove_path(gz), transition="round")
    body = body.cut(groove)

# ---------------- ribs on the inner faces of the side walls ----------------
for s in (-1, 1):
    xw = s * (W / 2.0 - TW - RIB_P / 2.0)
    for rz in RIB_Z:
        rib = (
            cq.Workplane("XY")
            .box(RIB_P, RIB_Y1 - RIB_Y0, RIB_H)
            .translate((xw, (RIB_Y0 + RIB_Y1) / 2.0, rz))
        )
        body = body.union(rib)

# ---------------- back wall cut-outs ----------------
for cx, w, z0, z1 in BACK_CUTS:
    c = (
        cq.Workplane("XZ", origin=(0, YB + 1.0, 0))
        .center(cx, (z0 + z1) / 2.0)
        .rect(w, z1 - z0)
        .extrude(TW + 2.0)
        .edges("|Y")
        .fillet(CUT_R)
    )
    body = body.cut(c)

# ---------------- floor: countersunk arc slot and hole ----------------
# the slot is an arc centred on the pivot hole (angular adjustment slot)
SLOT_R = HOLE_X - SLOT_X
SLOT_A = (SLOT_L - SLOT_W) / 2.0 / SLOT_R      # half angle of the slot centre line


def arc_slot(z, w):
    cx, cy, R, a = HOLE_X, HOLE_Y, SLOT_R, SLOT_A
    ro, ri = R + w / 2.0, R - w / 2.0

    def P(ang, r):
        return (cx + r * math.cos(ang), cy + r * math.sin(ang))

    def cap(ang, sgn):
        c = P(ang, R)
        return (c[0] - sgn * (w / 2.0) * math.sin(ang), c[1] + sgn * (w / 2.0) * math.cos(ang))

    a0, a1 = math.pi - a, math.pi + a
    return (
        cq.Workplane("XY", origin=(0, 0, z))
        .moveTo(*P(a0, ro))
        .threePointArc(P(math.pi, ro), P(a1, ro))
        .threePointArc(cap(a1, 1), P(a1, ri))
        .threePointArc(P(math.pi, ri), P(a0, ri))
        .threePointArc(cap(a0, -1), P(a0, ro))
        .close()
    )


body = body.cut(arc_slot(-1.0, SLOT_W).extrude(TF + 2.0))
csk_top = arc_slot(TF + 0.01, SLOT_W + 2 * CSK + 0.02).wires().val()
csk_bot = arc_slot(TF - CSK, SLOT_W).wires().val()
body = body.cut(cq.Workplane("XY").add(cq.Solid.makeLoft([csk_bot, csk_top], True)))

body = body.cut(
    cq.Workplane("XY", origin=(HOLE_X, HOLE_Y, -1.0)).circle(HOLE_D / 2.0).extrude(TF + 2.0)
)
body = body.cut(
    cq.Workplane("XY", origin=(HOLE_X, HOLE_Y, TF + 0.01))
    .circle(HOLE_D / 2.0 + CSK_H)
    .extrude(-CSK_H - 0.01, taper=45)
)

# ---------------- engraved lettering "KV_2A" (stroke letters) ----------------
# letter geometry in units of cap height, origin at K stem / baseline
LINES = [
    # K
    ((0.0, -0.2), (0.0, 1.2)),
    ((0.05, 0.57), (0.52 + 0.2 * 0.47 / 0.43, 1.2)),
    ((0.05, 0.57), (0.547 + 0.2 * 0.497 / 0.57, -0.2)),
    # V
    ((0.766 - 0.2 * 0.359 / 0.98, 1.2), (1.125, 0.02)),
    ((1.125, 0.02), (1.484 + 0.2 * 0.359 / 0.98, 1.2)),
    # 2 : diagonal and base
    ((2.885, 0.482), (2.404, 0.055)),
    ((2.404, 0.055), (3.004, 0.055)),
    # A
    ((3.184 - 0.2 * 0.422 / 0.957, -0.2), (3.606, 0.957)),
    ((3.606, 0.957), (4.012 + 0.2 * 0.406 / 0.957, -0.2)),
    ((3.184 + 0.371 * 0.422 / 0.957, 0.371), (4.012 - 0.371 * 0.406 / 0.957, 0.371)),
]
ARC2 = ((2.689, 0.703), 0.295, -48.4, 180.0)   # centre, radius, start/end angle (deg)
USCORE = (1.566, 2.316, -0.12)                 # x0, x1, centre height


def text_cutter():
    k = TEXT_CAP
    zb = TF - TEXT_DEPTH
    hgt = TEXT_DEPTH + 1.0

    def T(p):
        return (TEXT_X0 + p[0] * k, TEXT_BASE_Y + p[1] * k)

    solids = []
    for p0, p1 in LINES:
        a, b = T(p0), T(p1)
        dx, dy = b[0] - a[0], b[1] - a[1]
        ln = math.hypot(dx, dy)
        solids.append(
            cq.Workplane("XY", origin=((a[0] + b[0]) / 2.0, (a[1] + b[1]) / 2.0, zb))
            .slot2D(ln + TEXT_STROKE, TEXT_STROKE, angle=math.degrees(math.atan2(dy, dx)))
            .extrude(hgt)
        )
    (cu, cv), r, ang0, ang1 = ARC2
    c = T((cu, cv))
    ro, ri = r * k + TEXT_STROKE / 2.0, r * k - TEXT_STROKE / 2.0
    am = math.radians((ang0 + ang1) / 2.0)
    a0, a1 = math.radians(ang0), math.radians(ang1)

    def P(ang, rr):
        return (c[0] + rr * math.cos(ang), c[1] + rr * math.sin(ang))

    arc = (
        cq.Workplane("XY", origin=(0, 0, zb))
        .moveTo(*P(a0, ro))
        .threePointArc(P(am, ro), P(a1, ro))
        .lineTo(*P(a1, ri))
        .threePointArc(P(am, ri), P(a0, ri))
        .close()
        .extrude(hgt)
    )
    arc = arc.union(
        cq.Workplane("XY", origin=(P(a1, r * k)[0], P(a1, r * k)[1], zb))
        .circle(TEXT_STROKE / 2.0)
        .extrude(hgt)
    )
    letters = solids[0]
    for sld in solids[1:]:
        letters = letters.union(sld)
    band = (
        cq.Workplane("XY", origin=(TEXT_X0 + 2.0 * k, TEXT_BASE_Y + 0.5 * k, zb))
        .rect(6.0 * k, k)
        .extrude(hgt)
    )
    letters = letters.intersect(band)
    u0, u1, uv = USCORE
    us = (
        cq.Workplane("XY", origin=(TEXT_X0 + (u0 + u1) / 2.0 * k, TEXT_BASE_Y + uv * k, zb))
        .rect((u1 - u0) * k, TEXT_STROKE)
        .extrude(hgt)
    )
    return letters.union(us).union(arc)


body = body.cut(text_cutter())

result = body
